import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
D_OUT = 201.0        # tube outer diameter
WALL = 4.7           # tube wall thickness
H = 213.0            # tube height
FLOOR_T = 1.7        # bottom plate thickness (flush with tube bottom)
GAP_START = 190.0    # open sector in the floor: start angle (deg, CCW from +X)
GAP_END = 270.0      # open sector end angle (80 deg opening)
HUB_D = 48.8         # central hub disc diameter
HUB_DOWN = 0.9       # hub protrusion below the tube bottom
HUB_UP = 1.1         # hub protrusion above the floor
BOSS_D = 15.0        # central boss (underside) diameter
BOSS_DOWN = 6.5      # boss protrusion below the tube bottom
COLLAR_D = 12.3      # small collar on top of the hub
COLLAR_UP = 1.5      # collar height above hub top
BORE_D = 5.2         # central through-hole
CB_D = 10.5          # shallow counterbore at the boss bottom
CB_DEPTH = 1.5       # counterbore depth
SMALL_D = 3.5        # small holes in the hub (4 arms x 3)
SMALL_R = [11.4, 16.3, 21.0]  # radial positions of the small holes
HUB_X = 0.3          # hub centre offset from the tube axis (as measured)
HUB_Y = 0.65
SEAM_ANGLE = 225.0   # where cylindrical seams sit (cosmetic only)

R_OUT = D_OUT / 2.0
R_IN = R_OUT - WALL


def cyl(d, z0, h, x=0.0, y=0.0):
    """Vertical cylinder of diameter d from z0 to z0+h centred at (x, y)."""
    s = (cq.Workplane("XY").workplane(offset=z0)
         .circle(d / 2.0).extrude(h)
         .rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE))
    return s.translate((x, y, 0))


# ---------------- tube ----------------
tube = cyl(D_OUT, 0.0, H).cut(cyl(2 * R_IN, -1.0, H + 2.0))

# ---------------- floor with open sector ----------------
floor = cyl(2 * R_IN + 0.02, 0.0, FLOOR_T)

a0 = math.radians(GAP_START)
a1 = math.radians(GAP_END)
am = 0.5 * (a0 + a1)
rr = R_OUT * 1.5
wedge = (cq.Workplane("XY").workplane(offset=-FLOOR_T)
         .moveTo(0, 0)
         .lineTo(rr * math.cos(a0), rr * math.sin(a0))
         .threePointArc((rr * math.cos(am), rr * math.sin(am)),
                        (rr * math.cos(a1), rr * math.sin(a1)))
         .close()
         .extrude(FLOOR_T * 3))
floor = floor.cut(wedge)

# ---------------- hub disc, underside boss and top collar ----------------
hub_top = FLOOR_T + HUB_UP
hub = cyl(HUB_D, -HUB_DOWN, HUB_DOWN + hub_top, HUB_X, HUB_Y)
boss = cyl(BOSS_D, -BOSS_DOWN, BOSS_DOWN, HUB_X, HUB_Y)
collar = cyl(COLLAR_D, hub_top, COLLAR_UP, HUB_X, HUB_Y)

body = tube.union(floor).union(hub).union(boss).union(collar)

# ---------------- holes ----------------
z0 = -BOSS_DOWN - 5.0
cut_h = BOSS_DOWN + hub_top + COLLAR_UP + 10.0

pts = []
for k in range(4):
    ang = math.radians(90.0 * k)
    for r in SMALL_R:
        pts.append((HUB_X + r * math.cos(ang), HUB_Y + r * math.sin(ang)))
holes = (cq.Workplane("XY").workplane(offset=z0)
         .pushPoints(pts).circle(SMALL_D / 2.0).extrude(cut_h))

bore = cyl(BORE_D, z0, cut_h, HUB_X, HUB_Y)
cbore = cyl(CB_D, -BOSS_DOWN - 1.0, CB_DEPTH + 1.0, HUB_X, HUB_Y)

result = body.cut(holes).cut(bore).cut(cbore)

VIEW = {"azimuth": 45, "elevation": 26}
